import math
import cadquery as cq

# ---------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------
ZT = 28.6        # half height of main block / motor flange
ZH = 39.8        # half height of rear wall (horns)
XL = 70.8        # overall length along X
YF = 42.6        # front face of main block (clip face)
YW = 70.6        # front face of rear wall
YB = 77.2        # rear face
XB = 15.6        # -X face of rear block
YFE = 51.2       # +Y end of the motor flange
R_IN = 6.5       # inside corner round flange -> rear block
R_HF = 11.2      # concave round between top face and rear wall
R_TOP = 4.0      # rounding of rear wall top corners

# motor flange
TF = 9.1         # flange thickness (X)
CH_X = 4.5       # chamfer size in X
CH_Z = 5.0       # chamfer size in Z
PK_Y0 = 4.4      # pocket start (Y)
PK_Z = 18.9      # pocket half height
PK_FLOOR = 4.6   # pocket floor X position
MOT_Y = 24.05    # motor axis Y
MOT_D = 32.7     # centre bore
MOT_HOLE = 3.0   # motor screw holes
MOT_SP = 31.0    # motor screw spacing

# trough (big half bore along X)
TR_Y = 64.0
TR_R = 19.8
TR_OPEN = 15.9   # half width of the rear opening of the trough

# vertical U slots
U_X = (31.4, 54.9)
U_R = 7.1
U_YC = 58.4
NOTCH_Z = 26.6   # notch through rear wall, half height

# counterbored holes in rear wall (along Y)
CB_Z = 34.3
CB_D = 9.0
CB_DEPTH = 2.5
CB_HOLE = 3.5

# holes along X
XH_D = 3.9
XH_Z = 23.5
XH_Y = (47.2, 71.5)

# belt clip tabs on the front face
TAB_A = (26.4, 35.5)
TAB_B = (39.7, 48.8)
TAB_C = (52.9, XL)
LIP_Y = 36.5     # front of the cradle lips
LIP_TOP = 18.7
TAB_BOT = 12.9
LIP_R = 3.8
KN_Y = 31.8      # front of the centre knuckle
KN_R = 3.3
KN_FLAT = 36.2   # end of flat underside before ramp
RAMP_Z = 13.7    # ramp end on body face
KN_HOLE_Y = 37.3
KN_HOLE_Z = 24.1
KN_HOLE_D = 4.0


def arc_mid(c, r, ang_deg):
    a = math.radians(ang_deg)
    return (c[0] + r * math.cos(a), c[1] + r * math.sin(a))


# ---------------------------------------------------------------
# Main body: plan (XY) extrusion intersected with side (YZ) profile
# ---------------------------------------------------------------
c_in = (XB - R_IN, YFE + R_IN)
plan = (
    cq.Workplane("XY")
    .moveTo(0, YF)
    .lineTo(XL, YF)
    .lineTo(XL, YB)
    .lineTo(XB, YB)
    .lineTo(XB, YFE + R_IN)
    .threePointArc(arc_mid(c_in, R_IN, -45), (XB - R_IN, YFE))
    .lineTo(0, YFE)
    .close()
    .extrude(2 * ZH)
    .translate((0, 0, -ZH))
)

c_top = (YW - R_HF, ZT + R_HF)
c_bot = (YW - R_HF, -ZT - R_HF)
z_hf = min(ZT + R_HF, ZH)          # where the concave round meets the wall
side = (
    cq.Workplane("YZ")
    .moveTo(YF, -ZT)
    .lineTo(YW - R_HF, -ZT)
    .threePointArc(arc_mid(c_bot, R_HF, 45), (YW, -z_hf))
)
if ZH - z_hf > 1e-3:
    side = side.lineTo(YW, -ZH)
side = side.lineTo(YB, -ZH).lineTo(YB, ZH)
if ZH - z_hf > 1e-3:
    side = side.lineTo(YW, ZH)
side = (
    side.lineTo(YW, z_hf)
    .threePointArc(arc_mid(c_top, R_HF, -45), (YW - R_HF, ZT))
    .lineTo(YF, ZT)
    .close()
    .extrude(XL)
)

body = plan.intersect(side)

# round the top/bottom corners of the rear wall (edges along Y)
for xs in (XB, XL):
    for zs in (ZH, -ZH):
        body = body.edges(
            cq.selectors.BoxSelector(
                (xs - 0.5, YW + 0.5, zs - 0.5), (xs + 0.5, YB - 0.5, zs + 0.5)
            )
        ).fillet(R_TOP)

# ---------------------------------------------------------------
# Motor flange (X thickness TF, extends to -Y) with chamfered rim
# ---------------------------------------------------------------
flange = (
    cq.Workplane("XZ")
    .polyline(
        [
            (0, -ZT),
            (TF - CH_X, -ZT),
            (TF, -ZT + CH_Z),
            (TF, ZT - CH_Z),
            (TF - CH_X, ZT),
            (0, ZT),
        ]
    )
    .close()
    .extrude(-YF)
)
# pocket for the motor face
pocket = (
    cq.Workplane("XY")
    .box(TF, YF - PK_Y0, 2 * PK_Z, centered=False)
    .translate((PK_FLOOR, PK_Y0, -PK_Z))
)
flange = flange.cut(pocket)

body = body.union(flange)

# ---------------------------------------------------------------
# Belt clip tabs on the front face (upper set, mirrored to lower)
# ---------------------------------------------------------------
r_cr = YF - LIP_Y                 # concave cradle radius (tangent to body face)
CRADLE_TOP = LIP_TOP + r_cr       # where the cradle leaves the body face


def cradle(x0, x1):
    return (
        cq.Workplane("YZ")
        .moveTo(YF, TAB_BOT)
        .lineTo(YF, CRADLE_TOP)
        .threePointArc(arc_mid((LIP_Y, CRADLE_TOP), r_cr, -45), (LIP_Y, LIP_TOP))
        .lineTo(LIP_Y, TAB_BOT + LIP_R)
        .threePointArc(
            arc_mid((LIP_Y + LIP_R, TAB_BOT + LIP_R), LIP_R, 225),
            (LIP_Y + LIP_R, TAB_BOT),
        )
        .close()
        .extrude(x1 - x0)
        .translate((x0, 0, 0))
    )


def knuckle(x0, x1):
    k = (
        cq.Workplane("YZ")
        .moveTo(YF, RAMP_Z)
        .lineTo(YF, ZT)
        .lineTo(KN_Y + KN_R, ZT)
        .threePointArc(arc_mid((KN_Y + KN_R, ZT - KN_R), KN_R, 135), (KN_Y, ZT - KN_R))
        .lineTo(KN_Y, LIP_TOP)
        .lineTo(KN_FLAT, LIP_TOP)
        .close()
        .extrude(x1 - x0)
        .translate((x0, 0, 0))
    )
    hole = (
        cq.Workplane("YZ")
        .center(KN_HOLE_Y, KN_HOLE_Z)
        .circle(KN_HOLE_D / 2)
        .extrude(x1 - x0 + 2)
        .translate((x0 - 1, 0, 0))
    )
    return k.cut(hole)


tabs = cradle(*TAB_A).union(knuckle(*TAB_B)).union(cradle(*TAB_C))
tabs = tabs.union(tabs.mirror("XY"))
body = body.union(tabs)

# ---------------------------------------------------------------
# Cuts
# ---------------------------------------------------------------
# big trough along X
trough = (
    cq.Workplane("YZ")
    .center(TR_Y, 0)
    .circle(TR_R)
    .extrude(XL + 20)
    .translate((-10, 0, 0))
)
trough_open = (
    cq.Workplane("XY")
    .box(XL + 20, YB - TR_Y + 5, 2 * TR_OPEN, centered=False)
    .translate((-10, TR_Y, -TR_OPEN))
)
body = body.cut(trough).cut(trough_open)

# vertical U slots and notches through the rear wall
for xc in U_X:
    uslot = (
        cq.Workplane("XY")
        .center(xc, U_YC)
        .circle(U_R)
        .extrude(2 * ZH + 10)
        .translate((0, 0, -ZH - 5))
    )
    ubox = (
        cq.Workplane("XY")
        .box(2 * U_R, YW - U_YC, 2 * ZH + 10, centered=False)
        .translate((xc - U_R, U_YC, -ZH - 5))
    )
    notch = (
        cq.Workplane("XY")
        .box(2 * U_R, YB - YW + 2, 2 * NOTCH_Z, centered=False)
        .translate((xc - U_R, YW - 0.5, -NOTCH_Z))
    )
    body = body.cut(uslot).cut(ubox).cut(notch)

    # counterbored holes through the rear wall (along Y)
    for zs in (CB_Z, -CB_Z):
        h = (
            cq.Workplane("XZ")
            .center(xc, zs)
            .circle(CB_HOLE / 2)
            .extrude(-(YB - YW + 2))
            .translate((0, YW - 1, 0))
        )
        cb = (
            cq.Workplane("XZ")
            .center(xc, zs)
            .circle(CB_D / 2)
            .extrude(-(CB_DEPTH + 1))
            .translate((0, YW - 1, 0))
        )
        body = body.cut(h).cut(cb)

# motor centre bore and screw holes (along X through flange)
mot = (
    cq.Workplane(cq.Plane((0, MOT_Y, 0), (0, -1, 0), (1, 0, 0)))
    .circle(MOT_D / 2)
    .extrude(TF + 2)
    .translate((-1, 0, 0))
)
body = body.cut(mot)
for dy in (-MOT_SP / 2, MOT_SP / 2):
    for dz in (-MOT_SP / 2, MOT_SP / 2):
        mh = (
            cq.Workplane("YZ")
            .center(MOT_Y + dy, dz)
            .circle(MOT_HOLE / 2)
            .extrude(TF + 2)
            .translate((-1, 0, 0))
        )
        body = body.cut(mh)

# long holes along X
for yh in XH_Y:
    for zs in (XH_Z, -XH_Z):
        xh = (
            cq.Workplane("YZ")
            .center(yh, zs)
            .circle(XH_D / 2)
            .extrude(XL + 20)
            .translate((-10, 0, 0))
        )
        body = body.cut(xh)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
